import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# base / mounting block (origin = axis of the bottom boss, Z=0 = base underside)
BASE_X0 = -50.6          # left side of base
BASE_Y_BACK = 35.8       # back side of base
PLAT_Y_FRONT = -16.5     # front face of plateau
BASE_H_TOP = 27.1        # plateau height

# bottom boss (axis Z at origin)
BOSS_R, BOSS_H = 22.0, 8.0
BOSS2_R, BOSS2_H = 15.0, 2.0

# front housing (profile in XZ)
C1 = (30.25, 64.6)       # centre of the upper arc (also gear / motor axis)
R1 = 33.5
R2 = 22.5
R3 = 69.4
H_Y0, H_Y1 = -26.6, -2.8  # front / back face of housing
H_CH = 10.0             # radial width of the bevel
H_CH_Y = 3.5            # depth of the bevel

# ring boss on housing front
RING_R, RING_H = 18.4, 2.1
RING_MID_R, RING_IN_R = 11.25, 7.4

# rear body (motor/gear case)
REAR_Y0, REAR_Y1 = -18.0, 22.1
REAR_CH = 3.5

# upright connector
UC_X, UC_Y = -35.0, -5.7
UC_W = 20.0
UC_NOTCH = 2.2
UC_CYL_Y = -7.0
UC_TOP = 57.4
UC_CYL_R, UC_CYL_TOP = 8.0, 67.4

# side connector
SC_X0, SC_X1 = 36.5, 57.75
SC_Z0, SC_Z1 = 8.8, 28.7
SC_Y0, SC_Y1 = 2.2, 27.1
SC_END_Y1 = 37.7

# lower lobe (cylinder, axis Y)
LOBE_C = (46.9, 18.1)
LOBE_R = 15.5
LOBE_Y0 = -14.9

VIEW = {"azimuth": 45, "elevation": 26}


def xz_solid(wp_fn, y_front, y_back):
    """Build a 2D profile in the XZ plane and extrude it from y_back to y_front."""
    wp = cq.Workplane(cq.Plane(origin=(0, y_back, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))
    return wp_fn(wp).extrude(y_back - y_front)


def circ_tangent_internal(c_small, c_big, r_big):
    dx, dz = c_small[0] - c_big[0], c_small[1] - c_big[1]
    d = math.hypot(dx, dz)
    return (c_big[0] + r_big * dx / d, c_big[1] + r_big * dz / d)


# ---------- housing profile ----------
X_RIGHT = C1[0] + R1
Z_BOTTOM = 11.5
C2 = (X_RIGHT - R2, Z_BOTTOM + R2)


def solve_c3():
    a, b = R3 - R1, R3 - R2
    dx, dz = C2[0] - C1[0], C2[1] - C1[1]
    d = math.hypot(dx, dz)
    l = (a * a - b * b + d * d) / (2 * d)
    h = math.sqrt(max(a * a - l * l, 0.0))
    px, pz = C1[0] + l * dx / d, C1[1] + l * dz / d
    s1 = (px + h * dz / d, pz - h * dx / d)
    s2 = (px - h * dz / d, pz + h * dx / d)
    return s1 if s1[0] > s2[0] else s2


C3 = solve_c3()
T13 = circ_tangent_internal(C1, C3, R3)
T32 = circ_tangent_internal(C2, C3, R3)


def housing_outline_points():
    """Points on the cover outline: upper arc C1, large lower-left arc C3,
    lower-right corner arc C2 and the straight right-hand side."""
    def arc_pts(c, r, p, q, n):
        a0 = math.atan2(p[1] - c[1], p[0] - c[0])
        a1 = math.atan2(q[1] - c[1], q[0] - c[0])
        while a1 <= a0:
            a1 += 2 * math.pi
        return [(c[0] + r * math.cos(a0 + (a1 - a0) * k / n),
                 c[1] + r * math.sin(a0 + (a1 - a0) * k / n)) for k in range(n)]
    p_r1 = (X_RIGHT, C1[1])
    p_r2 = (X_RIGHT, C2[1])
    pts = arc_pts(C2, R2, T32, p_r2, 4)      # start low down where the seam is hidden
    pts += [(X_RIGHT, C2[1] + (C1[1] - C2[1]) * k / 3.0) for k in range(3)]
    pts += arc_pts(C1, R1, p_r1, T13, 8)
    pts += arc_pts(C3, R3, T13, T32, 4)
    return pts


# cover body: one smooth closed outline, shallow bevel all round front and back
housing = (cq.Workplane(cq.Plane(origin=(0, H_Y1, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))
           .spline(housing_outline_points(), periodic=True).close().extrude(H_Y1 - H_Y0))
housing = housing.faces("<Y or >Y").edges().chamfer(H_CH_Y, H_CH)


def front_wp(y, cx=0.0, cz=0.0, outward=True):
    n = (0, -1, 0) if outward else (0, 1, 0)
    return cq.Workplane(cq.Plane(origin=(cx, y, cz), xDir=(1, 0, 0), normal=n))


# ring boss on the front face with a two step recess
ring = front_wp(H_Y0 + 0.5, *C1).circle(RING_R).extrude(RING_H + 0.5)
ring = ring.faces("<Y").edges().chamfer(0.6)
housing = housing.union(ring)
ring_front = H_Y0 - RING_H
housing = housing.cut(front_wp(ring_front, *C1, outward=False).circle(RING_MID_R).extrude(1.2))
housing = housing.cut(front_wp(ring_front + 1.2, *C1, outward=False).circle(RING_IN_R).extrude(1.5))


# C-shaped tab (annular sector) on the housing front
def c_tab_profile(wp):
    r_in, r_out = 20.9, 27.2
    a0, a1 = math.radians(217), math.radians(263)
    am = 0.5 * (a0 + a1)
    P = lambda r, a: (C1[0] + r * math.cos(a), C1[1] + r * math.sin(a))
    return (wp.moveTo(*P(r_in, a0)).lineTo(*P(r_out, a0))
            .threePointArc(P(r_out, am), P(r_out, a1))
            .lineTo(*P(r_in, a1))
            .threePointArc(P(r_in, am), P(r_in, a0)).close())


c_tab = xz_solid(c_tab_profile, H_Y0 - 5.5, H_Y0 + H_CH_Y)
housing = housing.union(c_tab)

# ear with mounting hole (plate in XZ plane), thickened at its root
EAR_C = (-1.0, 86.4)
EAR_R = 7.2
EAR_HOLE_R = 3.9
EAR_ROOT = (-2.9, 71.7)          # where the ear's lower edge meets the housing
EAR_TOP_END = (14.0, 95.2)
EAR_Y0, EAR_Y1 = -10.2, -6.0
BRACKET_Y1 = -0.5


def ear_profile(wp):
    px, pz = EAR_ROOT
    dx, dz = EAR_C[0] - px, EAR_C[1] - pz
    d = math.hypot(dx, dz)
    ang = math.atan2(dz, dx) + math.asin(EAR_R / d)
    L = math.sqrt(d * d - EAR_R * EAR_R)
    t = (px + L * math.cos(ang), pz + L * math.sin(ang))
    a_t = math.atan2(t[1] - EAR_C[1], t[0] - EAR_C[0])
    if a_t < math.pi / 2:
        a_t += 2 * math.pi
    a_m = 0.5 * (a_t + math.pi / 2)
    mid = (EAR_C[0] + EAR_R * math.cos(a_m), EAR_C[1] + EAR_R * math.sin(a_m))
    top = (EAR_C[0], EAR_C[1] + EAR_R)
    return (wp.moveTo(*EAR_ROOT).lineTo(*t).threePointArc(mid, top)
            .lineTo(*EAR_TOP_END).lineTo(EAR_TOP_END[0], 66.0).lineTo(0.0, 62.0).close())


ear = xz_solid(ear_profile, EAR_Y0, EAR_Y1)
# supporting bracket under the ear, standing on the gear case
bracket = xz_solid(lambda wp: wp.polyline([(-3.2, 58.0), (-3.2, 72.0), (-5.6, 78.0), (0.0, 80.5), (4.0, 80.5),
                                           (4.0, 58.0)]).close(), EAR_Y0, BRACKET_Y1)
ear = ear.union(bracket)
ear = ear.cut(xz_solid(lambda wp: wp.center(*EAR_C).circle(EAR_HOLE_R), -12, 0))
housing = housing.union(ear)

# lower lobe (cylinder behind the housing bottom)
lobe = xz_solid(lambda wp: wp.center(*LOBE_C).circle(LOBE_R), LOBE_Y0, 0.0)

# ---------- rear body (gear case / motor can) ----------
# Ruled loft between a front section (vertical side, knee, straight 40 deg
# slope, crown over the motor axis, right flank) and a back section whose
# left side is steeper and rounder (tombstone shaped back plate).
REAR_Z_BOT = 12.0

REAR_FRONT_LEFT = [(-19.3, 40.5), (-18.4, 45.3), (-15.2, 49.4), (-10.0, 53.8), (-3.5, 59.4), (6.0, 68.6)]
REAR_BACK_LEFT = [(-17.9, 22.0), (-16.9, 29.0), (-12.8, 41.4), (-1.9, 58.3), (9.0, 70.2)]
MOTOR_C, MOTOR_R = C1, 19.5           # crown of the case is concentric with the output axis
CROWN_A0, CROWN_A1 = 125.0, -55.0     # deg, start / end of the crown arc
FLANK_DIR = (-0.30, -0.954)


def rear_section(y, left):
    pl = cq.Plane(origin=(0, y, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    P = lambda a: (MOTOR_C[0] + MOTOR_R * math.cos(math.radians(a)),
                   MOTOR_C[1] + MOTOR_R * math.sin(math.radians(a)))
    a0, a1 = CROWN_A0, CROWN_A1
    c0, c1, cm = P(a0), P(a1), P(0.5 * (a0 + a1))
    tan0 = (math.sin(math.radians(a0)), -math.cos(math.radians(a0)))
    t = (REAR_Z_BOT - c1[1]) / FLANK_DIR[1]
    flank_bot = (c1[0] + t * FLANK_DIR[0], REAR_Z_BOT)
    w = (cq.Workplane(pl).moveTo(flank_bot[0], REAR_Z_BOT).lineTo(left[0][0], REAR_Z_BOT)
         .lineTo(*left[0])
         .spline(left[1:] + [c0], tangents=[(0, 1), tan0], includeCurrent=True)
         .threePointArc(cm, c1)
         .close())
    return w.wires().val()


rear = cq.Workplane("XY").add(cq.Solid.makeLoft(
    [rear_section(REAR_Y0, REAR_FRONT_LEFT), rear_section(REAR_Y1, REAR_BACK_LEFT)], True))
rear = rear.faces(">Y").edges().chamfer(REAR_CH)
# three screws on the back face around the motor axis
SCREW_C, SCREW_PCR = (31.0, 63.0), 11.0
for a in (30.0, 150.0, 270.0):
    sx = SCREW_C[0] + SCREW_PCR * math.cos(math.radians(a))
    sz = SCREW_C[1] + SCREW_PCR * math.sin(math.radians(a))
    rear = rear.cut(cq.Workplane(cq.Plane(origin=(sx, REAR_Y1 + 0.1, sz), xDir=(1, 0, 0), normal=(0, -1, 0)))
                    .circle(1.4).extrude(1.2))

# two rectangular pads on the front face of the rear body (left of the housing)
PAD_ANG = -54.8
for (px, pz) in [(-6.6, 43.5), (0.6, 32.4)]:
    pad = (cq.Workplane(cq.Plane(origin=(px, REAR_Y0 + 0.5, pz), xDir=(1, 0, 0), normal=(0, -1, 0)))
           .transformed(rotate=(0, 0, PAD_ANG))
           .rect(12.8, 13.6).extrude(3.5))
    rear = rear.union(pad)

# ---------- base ----------
BF_C, BF_R = (7.6, 106.3), 139.0          # large arc forming the front of the base
BE_C, BE_A, BE_B = (1.0, 1.65), 32.5, 34.15  # elliptic right-hand part of the base
BASE_Z_BODY = 5.4                          # underside of the main base body
LEDGE_Z, LEDGE_SLOPE = 17.3, 0.12          # sloping ledge in front of plateau


def base_plan(z0, z1, y_min=-60.0, inset=0.0):
    h = z1 - z0
    rect = (cq.Workplane("XY").workplane(offset=z0)
            .center((BASE_X0 + inset + BE_C[0]) / 2, (-45.0 + BASE_Y_BACK - inset) / 2)
            .rect(BE_C[0] - BASE_X0 - inset, BASE_Y_BACK - inset + 45.0).extrude(h))
    rect = rect.edges("|Z and <X and >Y").fillet(17.0 - inset)
    front = (cq.Workplane("XY").workplane(offset=z0).center(*BF_C)
             .circle(BF_R - inset).extrude(h))
    rect = rect.intersect(front)
    ell = (cq.Workplane("XY").workplane(offset=z0).center(*BE_C)
           .ellipse(BE_A - inset, BE_B - inset).extrude(h))
    shape = rect.union(ell)
    if y_min > -60.0:
        shape = shape.intersect(cq.Workplane("XY").workplane(offset=z0 - 1)
                                .center(0, (y_min + 60.0) / 2).rect(200, 60.0 - y_min).extrude(h + 2))
    return shape


base_low = base_plan(BASE_Z_BODY, LEDGE_Z + 0.5)
base_low = base_low.edges("|Z").edges(cq.selectors.BoxSelector((-60, -40, -1), (-40, -10, 40))).fillet(3.0)
# sloping ledge in front of the plateau
ledge_cut = (cq.Workplane("YZ", origin=(-80, 0, 0))
             .polyline([(PLAT_Y_FRONT, LEDGE_Z), (-70.0, LEDGE_Z + LEDGE_SLOPE * (-70.0 - PLAT_Y_FRONT)),
                        (-70.0, 60.0), (PLAT_Y_FRONT, 60.0)]).close().extrude(160))
base_low = base_low.cut(ledge_cut)
plateau = base_plan(LEDGE_Z - 0.01, BASE_H_TOP, y_min=PLAT_Y_FRONT)
base = base_low.union(plateau)
# cove between plateau front face and lower step
try:
    base = base.edges(cq.selectors.BoxSelector((-55, PLAT_Y_FRONT - 0.5, LEDGE_Z - 0.5),
                                               (-20, PLAT_Y_FRONT + 0.5, LEDGE_Z + 0.5))).fillet(3.0)
except Exception:
    pass
# sloping top behind the gear case
BACK_SLOPE_Y0, BACK_SLOPE_Z1 = 22.5, 21.5
back_cut = (cq.Workplane("YZ", origin=(-80, 0, 0))
            .polyline([(BACK_SLOPE_Y0, BASE_H_TOP),
                       (60.0, BASE_H_TOP - (BASE_H_TOP - BACK_SLOPE_Z1) * (60.0 - BACK_SLOPE_Y0)
                        / (BASE_Y_BACK - BACK_SLOPE_Y0)),
                       (60.0, 60.0), (BACK_SLOPE_Y0, 60.0)]).close().extrude(160))
base = base.cut(back_cut)
# bottom plate
bplate = base_plan(2.6, BASE_Z_BODY + 0.01, inset=1.2)
base = base.union(bplate)
bround = cq.Workplane("XY").center(*BE_C).ellipse(BE_A - 0.6, BE_B - 0.6).extrude(BASE_Z_BODY)
base = base.union(bround)

boss = cq.Workplane("XY").circle(BOSS_R).extrude(-BOSS_H)
boss = boss.faces("<Z").edges().chamfer(0.8)
boss2 = cq.Workplane("XY").workplane(offset=-BOSS_H).circle(BOSS2_R).extrude(-BOSS2_H)
base = base.union(boss).union(boss2)

# small feet / tab on the underside and a pin at the back
for (px, py) in [(-43.0, 28.0), (-43.0, -12.0), (-12.0, 30.0), (12.0, -28.0)]:
    base = base.union(cq.Workplane("XY").workplane(offset=2.7).center(px, py).circle(1.6).extrude(-5.2))
foot = cq.Workplane("XY").workplane(offset=2.7).center(-43.0, 0.0).rect(7.5, 7.0).extrude(-5.6)
base = base.union(foot)
tab = cq.Workplane("XY").workplane(offset=0.3).center(-50.0, 0.0).rect(9.0, 4.6).extrude(-3.5)
base = base.union(tab)
pin = (cq.Workplane("XZ", origin=(0, BASE_Y_BACK - 0.5, 0)).center(0, 10.0)
       .circle(1.8).extrude(-4.4))
base = base.union(pin)

# ---------- upright connector ----------
uc_foot = (cq.Workplane("XY").workplane(offset=BASE_H_TOP).center(UC_X, UC_Y)
           .rect(UC_W + 4.6, UC_W + 4.6).extrude(4.0))
uc_foot = uc_foot.edges("|Z").chamfer(2.0)
uc_foot = uc_foot.faces(">Z").edges().chamfer(1.0)
uc_body = (cq.Workplane("XY").workplane(offset=BASE_H_TOP + 4).center(UC_X, UC_Y)
           .rect(UC_W, UC_W).extrude(UC_TOP - BASE_H_TOP - 4))
# notched vertical corners of the connector body
uc_body = uc_body.cut(cq.Workplane("XY").workplane(offset=BASE_H_TOP + 4).center(UC_X, UC_Y)
                      .rect(UC_W, UC_W, forConstruction=True).vertices()
                      .rect(2 * UC_NOTCH, 2 * UC_NOTCH).extrude(UC_TOP - BASE_H_TOP - 4))
uc_cyl = (cq.Workplane("XY").workplane(offset=UC_TOP).center(UC_X, UC_CYL_Y)
          .circle(UC_CYL_R).extrude(UC_CYL_TOP - UC_TOP))
uc_key = (cq.Workplane("XY").workplane(offset=UC_TOP).center(UC_X, UC_CYL_Y + UC_CYL_R + 0.85)
          .rect(8.2, 5.7).extrude(UC_CYL_TOP - UC_TOP))
upright = uc_foot.union(uc_body).union(uc_cyl).union(uc_key)

# ---------- side connector ----------
SC_XC = (SC_X0 + SC_X1) / 2
SC_UP_X0, SC_UP_X1, SC_STEP_Z = 40.1, 53.5, 25.3
sc_flange = (cq.Workplane("XZ", origin=(0, SC_Y0, 0)).center(SC_XC, (SC_Z0 + SC_Z1) / 2 + 0.5)
             .rect(SC_X1 - SC_X0 + 1.0, SC_Z1 - SC_Z0 + 2.0).extrude(SC_Y0 + 0.7))
sc_body = (cq.Workplane("XZ", origin=(0, SC_Y1, 0)).center(SC_XC, (SC_Z0 + SC_STEP_Z) / 2)
           .rect(SC_X1 - SC_X0, SC_STEP_Z - SC_Z0).extrude(SC_Y1 - SC_Y0))
sc_upper = (cq.Workplane("XZ", origin=(0, SC_Y1, 0)).center((SC_UP_X0 + SC_UP_X1) / 2, (SC_STEP_Z + SC_Z1) / 2)
            .rect(SC_UP_X1 - SC_UP_X0, SC_Z1 - SC_STEP_Z + 0.01).extrude(SC_Y1 - SC_Y0))
SC_END_C = (46.8, 19.4)
sc_end_cyl = (cq.Workplane("XZ", origin=(0, SC_END_Y1, 0)).center(*SC_END_C)
              .circle(8.0).extrude(SC_END_Y1 - SC_Y1 + 0.5))
sc_end_top = (cq.Workplane("XZ", origin=(0, SC_END_Y1, 0)).center(SC_END_C[0], 26.5)
              .rect(8.6, 6.2).extrude(SC_END_Y1 - SC_Y1 + 0.5))
side_conn = sc_flange.union(sc_body).union(sc_upper).union(sc_end_cyl).union(sc_end_top)

result = (base.union(rear).union(housing).union(lobe)
          .union(upright).union(side_conn))
